import math
import cadquery as cq

# =====================================================================
# Housing with nut traps, open back, bottom flange, C-ring spigot and
# two snap legs.  X = width, Y = depth (front face is -Y), Z = up (mm)
# =====================================================================

# ---------------- body (octagonal housing) ----------------
BX = 12.0          # half width of body
BY0 = -9.6         # front face
BY1 = 9.6          # back face
FF_HALF = 8.65     # half width of the flat front face
FCH_Y = -2.1       # y where the front chamfers meet the side faces
BCH_X = 2.0        # back chamfer size in X
BCH_Y = 4.4        # back chamfer size in Y
EDGE_R = 0.6       # small round on the outer vertical edges
TOP_R = 0.6        # small round on the top outer edges

# ---------------- heights ----------------
Z_LEG_BOT = 0.0
Z_HOOK_TOP = 3.0
Z_TUBE_BOT = 3.0
Z_WIN_TOP = 7.7     # top of the front window of the C-ring
Z_FL_BOT = 12.5
Z_FL_TOP = 16.25
Z_BODY_BOT = 19.0   # top of the sloped skirt
Z_STEP_BOT = 45.8   # back-right chamfer ends / slope starts
Z_STEP_TOP = 51.6   # slope reaches the square corner
Z_TOP = 74.2

# ---------------- flange ----------------
FL_HALF = 16.65
FL_CH_Y = -4.2     # y where the flange front chamfer meets its side
FL_R = 1.6         # back corner radius of flange
FL_R2 = 1.2        # radius where the flange front chamfer meets its side
FL_EDGE_R = 0.5    # round on the outer top edges of the flange

# ---------------- walls / cavity ----------------
T_SIDE = 3.2
T_UP = 0.6         # extra side wall thickness in the upper part of the cavity
Z_LEDGE = 53.5     # where the upper (thicker, square cornered) part of the cavity starts
LEDGE_H = 3.0      # height of the sloped transition
UP_CH = 1.5        # small inner chamfer in the front corners of the upper cavity
T_FRONT = 3.5
T_TOP = 3.0
Z_FLOOR = 14.2
CAV_R = 1.5        # inner fillet of the cavity

# ---------------- holes / spigot ----------------
AX_Y = 2.35                # y of the common axis of top hole, bore and spigot
TOP_HOLE_D = 7.3
TUBE_R = 8.72
BORE_R = 5.9
TUBE_CUT_Y = AX_Y - 4.06   # front window of the lower ring
TUBE_FILLET = 1.0

# ---------------- nut traps on the front face ----------------
HEX_X = 6.7
HEX_Z = (61.6, 17.0)
HEX_AF = 5.6       # across flats
HEX_DEPTH = 2.5
NUT_HOLE_D = 3.2

# ---------------- snap legs ----------------
LEG_X0 = 11.25
LEG_X1 = 14.3
LEG_Y0 = -2.3
LEG_Y1 = 7.4
HOOK_OUT = 1.0
HOOK_R = 0.95

# ---------------- lid groove at the back of the +X wall (shows as a notch on top) ----------------
NOTCH_X0 = 12.0 - T_SIDE - T_UP   # inner side = inner face of the upper cavity
NOTCH_X1 = 10.9
NOTCH_Y0 = 6.7


# =====================================================================
# helpers
# =====================================================================
def poly_body(back_right_chamfer):
    pts = [(-FF_HALF, BY0), (FF_HALF, BY0), (BX, FCH_Y)]
    if back_right_chamfer:
        pts += [(BX, BY1 - BCH_Y), (BX - BCH_X, BY1)]
    else:
        pts += [(BX, BY1)]
    pts += [(-BX + BCH_X, BY1), (-BX, BY1 - BCH_Y), (-BX, FCH_Y)]
    return pts


def offset_polygon(pts, dists):
    """Offset a CCW convex polygon inward; dists[i] is the offset of edge i (pts[i] -> pts[i+1])."""
    n = len(pts)
    lines = []
    for i in range(n):
        x0, y0 = pts[i]
        x1, y1 = pts[(i + 1) % n]
        dx, dy = x1 - x0, y1 - y0
        L = math.hypot(dx, dy)
        nx, ny = -dy / L, dx / L          # inward normal for CCW polygon
        d = dists[i]
        lines.append(((x0 + nx * d, y0 + ny * d), (dx, dy)))
    out = []
    for i in range(n):
        (p1, d1) = lines[i - 1]
        (p2, d2) = lines[i]
        den = d1[0] * d2[1] - d1[1] * d2[0]
        t = ((p2[0] - p1[0]) * d2[1] - (p2[1] - p1[1]) * d2[0]) / den
        out.append((p1[0] + d1[0] * t, p1[1] + d1[1] * t))
    return out


def prism(pts, z0, z1):
    return cq.Workplane("XY").workplane(offset=z0).polyline(pts).close().extrude(z1 - z0)


def unit(v):
    L = math.sqrt(sum(c * c for c in v))
    return tuple(c / L for c in v)


def cross(u, v):
    return (u[1] * v[2] - u[2] * v[1], u[2] * v[0] - u[0] * v[2], u[0] * v[1] - u[1] * v[0])


def halfspace(point, normal, size=200.0):
    """Big block on the -normal side of the plane through point."""
    nrm = cq.Vector(*normal)
    xd = nrm.cross(cq.Vector(0, 0, 1))
    if xd.Length < 1e-6:
        xd = cq.Vector(1, 0, 0)
    pl = cq.Plane(origin=cq.Vector(*point), xDir=xd, normal=nrm)
    return cq.Workplane(pl).rect(size, size).extrude(-size)


# back-right chamfer (lower part) and its planar sloped transition
CH_P = (BX, BY1 - BCH_Y, Z_STEP_BOT)
CH_Q = (BX - BCH_X, BY1, Z_STEP_BOT)
CH_S = (BX, BY1, Z_STEP_TOP)
_n = cross(tuple(q - p for q, p in zip(CH_Q, CH_P)), tuple(s_ - p for s_, p in zip(CH_S, CH_P)))
SLOPE_N = unit(tuple(-c for c in _n))                     # points up / inward
CH_N = unit((BCH_Y, BCH_X, 0.0))                          # outward normal of the back-right chamfer


def corner_region(shift):
    """Region behind the back-right chamfer plane and below the slope plane, moved inward (-X) by shift."""
    a = halfspace(CH_P, tuple(-c for c in CH_N))
    b = halfspace(CH_P, SLOPE_N)
    box = cq.Workplane("XY").box(40, 40, 120, centered=(True, True, False)).translate((BX, BY1, -10))
    return box.intersect(a).intersect(b).translate((-shift, 0, 0))


# =====================================================================
# outer body
# =====================================================================
upper = poly_body(False)
lower = poly_body(True)

body = prism(upper, Z_BODY_BOT, Z_TOP)
body = body.edges("|Z").fillet(EDGE_R)
body = body.faces(">Z").edges().fillet(TOP_R)
body = body.cut(corner_region(0.0))

# flange whose top slopes up to the body outline at a constant angle (hip roof)
SKIRT_RUN = FL_HALF - BX                      # horizontal run of the slope on the sides
SKIRT_RISE = Z_BODY_BOT - Z_FL_TOP            # rise of the slope


def roof_plane(p0, p1):
    """Half space below the plane through the body edge p0->p1 (at Z_BODY_BOT) sloping down outward."""
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(dx, dy)
    nx, ny = dy / L, -dx / L                   # outward normal of a CCW polygon edge
    nrm = unit((nx * SKIRT_RISE, ny * SKIRT_RISE, SKIRT_RUN))
    return halfspace((p0[0], p0[1], Z_BODY_BOT), nrm)


flange = prism([(-FF_HALF, BY0), (FF_HALF, BY0), (FL_HALF, FL_CH_Y), (FL_HALF, BY1),
                 (-FL_HALF, BY1), (-FL_HALF, FL_CH_Y)], Z_FL_BOT, Z_BODY_BOT)
zm = 0.5 * (Z_FL_BOT + Z_BODY_BOT)
for sx in (-1, 1):
    flange = flange.edges(cq.selectors.NearestToPointSelector((sx * FL_HALF, BY1, zm))).fillet(FL_R)
    flange = flange.edges(cq.selectors.NearestToPointSelector((sx * FL_HALF, FL_CH_Y, zm))).fillet(FL_R2)
for i in range(len(lower)):
    p0, p1 = lower[i], lower[(i + 1) % len(lower)]
    if abs(p0[1] - p1[1]) < 1e-9:               # front and back edges: walls are flush, no slope
        continue
    flange = flange.intersect(roof_plane(p0, p1))
# soften the outer top edges of the flange (the ones that stay below the body)
fl_edges = [e for e in flange.edges().vals()
            if Z_FL_BOT + 0.5 < e.BoundingBox().zmin and e.BoundingBox().zmax < Z_BODY_BOT - 0.3]
flange = flange.newObject(fl_edges).fillet(FL_EDGE_R)
part = body.union(flange)

# =====================================================================
# cavity, open at the back; side walls thicker in the upper part
# =====================================================================
square = [(-FF_HALF, BY0), (FF_HALF, BY0), (BX, FCH_Y), (BX, BY1), (-BX, BY1), (-BX, FCH_Y)]
cav_lo = offset_polygon(square, [T_FRONT, T_SIDE, T_SIDE, -6.0, T_SIDE, T_SIDE])
XU = BX - T_SIDE - T_UP                       # half width of the upper cavity
YF = BY0 + T_FRONT                            # inner front face
cav_hi = [(-XU + UP_CH, YF), (XU - UP_CH, YF), (XU, YF + UP_CH), (XU, BY1 + 6.0), (-XU, BY1 + 6.0), (-XU, YF + UP_CH)]


def loft2(p0, z0, p1, z1):
    return (cq.Workplane("XY").workplane(offset=z0).polyline(p0).close()
            .workplane(offset=z1 - z0).polyline(p1).close().loft(ruled=True))


cav_a = prism(cav_lo, Z_FLOOR, Z_LEDGE).faces("<Z").edges().fillet(CAV_R)
cav_b = loft2(cav_lo, Z_LEDGE, cav_hi, Z_LEDGE + LEDGE_H)
cav_c = prism(cav_hi, Z_LEDGE + LEDGE_H, Z_TOP - T_TOP).faces(">Z").edges().fillet(CAV_R)
cavity = cav_a.union(cav_b).union(cav_c)
part = part.cut(cavity)

# top hole
part = part.cut(
    cq.Workplane("XY").workplane(offset=Z_TOP - T_TOP - 1).center(0, AX_Y).circle(TOP_HOLE_D / 2).extrude(T_TOP + 2)
)

# =====================================================================
# spigot below the flange: ring, front window in its lower part
# =====================================================================
tube = (
    cq.Workplane("XY").workplane(offset=Z_TUBE_BOT).center(0, AX_Y).circle(TUBE_R)
    .extrude(Z_FL_BOT - Z_TUBE_BOT + 0.5)
)
tube = tube.faces("<Z").edges().fillet(TUBE_FILLET)
win = cq.Workplane("XY").box(40, 40, Z_WIN_TOP - Z_TUBE_BOT + 1, centered=(True, False, False)).translate(
    (0, TUBE_CUT_Y - 40, Z_TUBE_BOT - 1))
tube = tube.cut(win)
part = part.union(tube)
part = part.cut(
    cq.Workplane("XY").workplane(offset=Z_TUBE_BOT - 1).center(0, AX_Y).circle(BORE_R)
    .extrude(Z_FLOOR - Z_TUBE_BOT + 2)
)

# =====================================================================
# snap legs with hooks
# =====================================================================
for s in (-1, 1):
    prof = (
        cq.Workplane("XZ")
        .moveTo(LEG_X0, Z_FL_BOT + 0.5)
        .lineTo(LEG_X0, Z_LEG_BOT)
        .lineTo(LEG_X1 + HOOK_OUT, Z_LEG_BOT)
        .lineTo(LEG_X1 + HOOK_OUT, Z_HOOK_TOP)
        .lineTo(LEG_X1, Z_HOOK_TOP)
        .lineTo(LEG_X1, Z_FL_BOT + 0.5)
        .close()
        .extrude(-(LEG_Y1 - LEG_Y0))
        .translate((0, LEG_Y0, 0))
    )
    prof = prof.edges("|Y").edges(
        cq.selectors.NearestToPointSelector((LEG_X1 + HOOK_OUT, 0, Z_LEG_BOT))).fillet(HOOK_R)
    if s < 0:
        prof = prof.mirror("YZ")
    part = part.union(prof)

# =====================================================================
# nut traps on the front face
# =====================================================================
R_HEX = HEX_AF / math.sqrt(3.0)    # circumradius, pointy top
for hz in HEX_Z:
    for sx in (-1, 1):
        hx = sx * HEX_X
        hpts = [(hx + R_HEX * math.cos(math.radians(90 + 60 * k)), hz + R_HEX * math.sin(math.radians(90 + 60 * k)))
                for k in range(6)]
        hexw = cq.Workplane("XZ").workplane(offset=-BY0 + 0.01).polyline(hpts).close().extrude(-(HEX_DEPTH + 0.01))
        part = part.cut(hexw)
        hole = (cq.Workplane("XZ").workplane(offset=-BY0 + 0.5).center(hx, hz)
                .circle(NUT_HOLE_D / 2).extrude(-(T_FRONT + 6)))
        part = part.cut(hole)

# =====================================================================
# groove for the lid at the back of the +X wall (upper part, open at the top)
# =====================================================================
groove = cq.Workplane("XY").box(NOTCH_X1 - NOTCH_X0 + 0.5, BY1 - NOTCH_Y0 + 1, Z_TOP - Z_STEP_BOT + 1,
                                centered=False).translate((NOTCH_X0 - 0.5, NOTCH_Y0, Z_STEP_BOT))
# the groove ends on a slope parallel to the outer step transition
groove = groove.intersect(halfspace(tuple(c - d for c, d in zip(CH_P, (BX - NOTCH_X1, 0, 0))),
                                    tuple(-c for c in SLOPE_N)))
part = part.cut(groove)

result = part
